import math
import cadquery as cq

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- driving dimensions (mm) ----------------
BOX_X = 72.0        # outer width of the box (X)
BOX_Y = 95.5        # outer depth of the box (Y)
H = 50.0            # overall height
WALL = 2.4          # wall thickness
BOX_R = 2.0         # outer vertical corner radius of the box
IN_R = 0.4          # inner vertical corner radius
FLOOR = 1.8         # floor thickness

FL_OFF = 10.2       # flange overhang beyond the walls
FL_EDGE = 2.0       # height of the vertical flange rim
FL_H = 8.4          # height where the sloped flange meets the wall
FL_EDGE_FIL = 0.6   # rounding of the flange rim
RIM_FIL = 1.1       # rounding of both top edges of the wall (nearly half-round rim)
NOTCH_FIL = 2.5     # rounding of the flange edges along the notch

# notch + cable window in the +Y side
NOTCH_W = 25.5
NOTCH_CX = 2.2      # notch is slightly off-centre towards +X
ARCH_TOP = 15.0     # top of the shallow arched recess on the wall
ARCH_R = 6.0        # corner radius of that recess
ARCH_DEPTH = 0.4    # depth of the recess into the wall
WIN_W = 22.0
WIN_Z0 = 2.4
WIN_H = 8.4

# side hole (+X side)
HOLE_D = 6.2
HOLE_Y = 34.7
HOLE_Z = 8.0
HOLE_DEPTH = 6.0    # measured inward from the outer wall face (breaks through the wall)
HOLE_TUBE = 0.6     # short tube around the hole on the inside of the wall (length)
HOLE_TUBE_T = 0.25  # its wall thickness

# floor guide (U shaped rib on the floor)
GUIDE_X_IN = 22.9
GUIDE_X_OUT = 25.7
GUIDE_Y_END = 23.7
GUIDE_BLOCK_Y = -31.0
GUIDE_H = 3.0

# rounded vertical rib inside the -Y wall
RIB_R = 11.0
RIB_SAG = 1.4
RIB_TOP_GAP = 2.6

# embossed letters "AT" on the inside of the -Y wall
TXT_H = 16.5        # letter height
TXT_Z0 = 11.4       # bottom of the letters
TXT_DEPTH = 0.7     # emboss height
TXT_STROKE = 2.8    # stroke width
A_W = 12.6          # width of the "A"
T_W = 11.4          # width of the "T"
A_CX = 20.8         # letter centres (x) on the wall
T_CX = 8.4

IX = BOX_X - 2 * WALL
IY = BOX_Y - 2 * WALL

# ---------------- body ----------------
FX = BOX_X + 2 * FL_OFF
FY = BOX_Y + 2 * FL_OFF
FR = BOX_R + FL_OFF


def rrect(wp, w, h, r):
    return wp.sketch().rect(w, h).vertices().fillet(r).finalize()


base = rrect(cq.Workplane("XY"), FX, FY, FR).extrude(FL_EDGE)

slope_h = FL_H - FL_EDGE
taper = math.degrees(math.atan2(FL_OFF, slope_h))
slope = rrect(cq.Workplane("XY", origin=(0, 0, FL_EDGE)), FX, FY, FR).extrude(slope_h, taper=taper)

flange = base.union(slope, clean=True)
# round the crease between the vertical flange band and the sloped top
flange = flange.edges(
    cq.selectors.BoxSelector((-FX, -FY, FL_EDGE - 0.01), (FX, FY, FL_EDGE + 0.01))
).fillet(FL_EDGE_FIL)

box = rrect(cq.Workplane("XY"), BOX_X, BOX_Y, BOX_R).extrude(H)

body = flange.union(box)

# interior cavity
cavity = rrect(cq.Workplane("XY", origin=(0, 0, FLOOR)), IX, IY, IN_R).extrude(H)
body = body.cut(cavity)

# round the top rim (outer and inner edge)
body = body.edges(cq.selectors.BoxSelector((-BOX_X, -BOX_Y, H - 0.01), (BOX_X, BOX_Y, H + 0.01))).fillet(RIM_FIL)

# ---------------- notch, arched recess and window on +Y side ----------------
notch = (
    cq.Workplane("XY", origin=(NOTCH_CX, BOX_Y / 2 + FL_OFF, -1))
    .rect(NOTCH_W, 2 * FL_OFF)
    .extrude(FL_H + 2)
)
body = body.cut(notch)


def notch_slope_edges(shape):
    # the sloped edges where the flange top meets the two notch side faces
    out = []
    for e in shape.edges().vals():
        bb = e.BoundingBox()
        for xs in (NOTCH_CX - NOTCH_W / 2, NOTCH_CX + NOTCH_W / 2):
            if (abs(bb.xmin - xs) < 1e-3 and abs(bb.xmax - xs) < 1e-3
                    and bb.zmax > FL_H - 0.5 and bb.zmin > 1.0 and bb.ymax - bb.ymin > FL_OFF / 2):
                out.append(e)
    return out


body = body.newObject(notch_slope_edges(body)).fillet(NOTCH_FIL)

# arched profile in the XZ plane, pushed a little into the wall
arch = (
    cq.Workplane("XZ", origin=(NOTCH_CX, BOX_Y / 2 + FL_OFF + 1, 0))
    .sketch()
    .push([(0, (ARCH_TOP - 1) / 2)])
    .rect(NOTCH_W, ARCH_TOP + 1)
    .reset()
    .vertices(">Y")
    .fillet(ARCH_R)
    .finalize()
    .extrude(FL_OFF + 1 + ARCH_DEPTH)
)
body = body.cut(arch)

window = (
    cq.Workplane("XY", origin=(NOTCH_CX, BOX_Y / 2, WIN_Z0))
    .rect(WIN_W, 4 * WALL)
    .extrude(WIN_H)
)
body = body.cut(window)

# ---------------- side hole on +X ----------------
tube = (
    cq.Workplane("YZ", origin=(IX / 2 - HOLE_TUBE, HOLE_Y, HOLE_Z))
    .circle(HOLE_D / 2 + HOLE_TUBE_T)
    .extrude(HOLE_TUBE + 0.2)
)
body = body.union(tube)
hole = (
    cq.Workplane("YZ", origin=(BOX_X / 2 - HOLE_DEPTH, HOLE_Y, HOLE_Z))
    .circle(HOLE_D / 2)
    .extrude(HOLE_DEPTH + FL_OFF + 2)
)
body = body.cut(hole)

# ---------------- floor guide ----------------
leg_w = GUIDE_X_OUT - GUIDE_X_IN
leg_len = GUIDE_Y_END + IY / 2 + 0.5
legs = (
    cq.Workplane("XY", origin=(0, 0, FLOOR - 0.1))
    .pushPoints([((GUIDE_X_IN + GUIDE_X_OUT) / 2 * s, GUIDE_Y_END - leg_len / 2) for s in (-1, 1)])
    .rect(leg_w, leg_len)
    .extrude(GUIDE_H + 0.1)
)
blk_len = GUIDE_BLOCK_Y + IY / 2 + 0.5
block = (
    cq.Workplane("XY", origin=(0, GUIDE_BLOCK_Y - blk_len / 2, FLOOR - 0.1))
    .rect(2 * GUIDE_X_OUT, blk_len)
    .extrude(GUIDE_H + 0.1)
)
body = body.union(legs).union(block)

# ---------------- rounded rib inside the -Y wall ----------------
rib = (
    cq.Workplane("XY", origin=(0, -IY / 2 - (RIB_R - RIB_SAG), FLOOR - 0.1))
    .circle(RIB_R)
    .extrude(H - RIB_TOP_GAP - FLOOR + 0.1)
)
# keep only the part between the middle of the wall and the inner bulge
rib_y0 = -IY / 2 - WALL / 2
rib_y1 = -IY / 2 + RIB_SAG + 0.1
rib = rib.intersect(
    cq.Workplane("XY", origin=(0, (rib_y0 + rib_y1) / 2, 0)).rect(2 * RIB_R, rib_y1 - rib_y0).extrude(H)
)
body = body.union(rib)

# ---------------- embossed "AT" ----------------
def a_profile(w, h, t):
    apex = 0.8 * t / 1.5            # half width of the flat apex
    k = (w / 2 - apex) / h          # inward lean of the legs per unit height
    cb0, cb1 = 0.21 * h, 0.34 * h   # crossbar bottom / top
    xi = lambda z: w / 2 - t - k * z  # inner edge of the right leg
    outer = [(-w / 2, 0), (-apex, h), (apex, h), (w / 2, 0), (w / 2 - t, 0),
             (xi(cb0), cb0), (-xi(cb0), cb0), (-(w / 2 - t), 0)]
    z_top = min((w / 2 - t) / k, h - t)
    if xi(z_top) < 0.05:   # legs meet: triangular counter
        counter = [(-xi(cb1), cb1), (xi(cb1), cb1), (0.0, z_top)]
    else:
        counter = [(-xi(cb1), cb1), (xi(cb1), cb1), (xi(z_top), z_top), (-xi(z_top), z_top)]
    return outer, counter


def t_profile(w, h, t):
    sw = t * 1.05 / 2
    return [(-w / 2, h), (w / 2, h), (w / 2, h - t), (sw, h - t), (sw, 0), (-sw, 0),
            (-sw, h - t), (-w / 2, h - t)]


def letter(poly, cx, hole_pts=None):
    # plane on the inner face of the -Y wall, normal +Y (into the box);
    # local x runs towards -X so the text reads correctly from inside
    pl = cq.Plane(origin=(cx, -IY / 2 - 0.1, TXT_Z0), xDir=(-1, 0, 0), normal=(0, 1, 0))
    w = cq.Workplane(pl).polyline(poly).close().extrude(TXT_DEPTH + 0.1)
    if hole_pts:
        w = w.cut(cq.Workplane(pl).polyline(hole_pts).close().extrude(TXT_DEPTH + 1))
    return w


A_out, A_in = a_profile(A_W, TXT_H, TXT_STROKE)
body = body.union(letter(A_out, A_CX, A_in)).union(letter(t_profile(T_W, TXT_H, TXT_STROKE), T_CX))

result = body
